import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_TEETH = 30          # number of teeth
MODULE = 2.0          # gear module
PRESSURE_ANGLE = 20.0 # degrees
THICKNESS = 10.0      # face width (overall gear thickness)
DEDENDUM_COEF = 1.15  # root depth below pitch circle, in modules
BACKLASH = 0.2        # tooth thinning at the pitch circle (mm)

RECESS_DIA = 49.2     # top recess (inside rim) diameter
RECESS_DEPTH = 2.8    # depth of recess from top face
HUB_DIA = 15.6        # central hub boss diameter
HUB_TOP_BELOW = 0.0   # hub top distance below rim top face (0 = flush)
BORE_DIA = 6.4        # central bore
HOLE_COUNT = 6        # lightening holes
HOLE_DIA = 11.3
HOLE_PCD_R = 16.3     # hole circle radius

# ---------------- gear geometry ----------------
rp = MODULE * N_TEETH / 2.0
ra = rp + MODULE
rf = rp - DEDENDUM_COEF * MODULE
alpha = math.radians(PRESSURE_ANGLE)
rb = rp * math.cos(alpha)


def inv(a):
    return math.tan(a) - a


# half tooth thickness angle at pitch circle
half_pitch_ang = math.pi / (2 * N_TEETH) - (BACKLASH / 2.0) / rp
inv_p = inv(alpha)


def flank_angle(r):
    """Angular half-thickness of the tooth at radius r (>= rb)."""
    r = max(r, rb)
    a_r = math.acos(rb / r)
    return half_pitch_ang + inv_p - inv(a_r)


def pol(r, a):
    return (r * math.cos(a), r * math.sin(a))


r_start = max(rb, rf)
N_FLANK = 6
flank_r = [r_start + (ra - r_start) * i / (N_FLANK - 1) for i in range(N_FLANK)]
pitch = 2 * math.pi / N_TEETH

wp = cq.Workplane("XY")
first = True
for i in range(N_TEETH):
    c = i * pitch
    # lower flank (clockwise side), going outward
    lower = [pol(r, c - flank_angle(r)) for r in flank_r]
    upper = [pol(r, c + flank_angle(r)) for r in reversed(flank_r)]
    root_lo = pol(rf, c - flank_angle(r_start))
    root_hi = pol(rf, c + flank_angle(r_start))
    if first:
        wp = wp.moveTo(*root_lo)
        first = False
    # single smooth flank face: radial run-in below the base circle + involute
    wp = wp.spline(lower, includeCurrent=True)
    wp = wp.threePointArc(pol(ra, c), upper[0])
    wp = wp.spline(upper[1:] + [root_hi], includeCurrent=True)
    # root arc to next tooth
    cn = c + pitch
    nxt = pol(rf, cn - flank_angle(r_start))
    mid = pol(rf, c + pitch / 2.0)
    if i == N_TEETH - 1:
        wp = wp.threePointArc(mid, pol(rf, -flank_angle(r_start)))
    else:
        wp = wp.threePointArc(mid, nxt)
wp = wp.close()
gear = wp.extrude(THICKNESS)

SEAM_ANG = 225.0  # start angle of full circles (puts cylinder seams on a silhouette)


def cyl(x, y, r, z0, h):
    """Plain cylinder, axis +Z, base at z0."""
    return (cq.Workplane("XY").workplane(offset=z0).center(x, y)
            .transformed(rotate=(0, 0, SEAM_ANG)).circle(r).extrude(h))


z_floor = THICKNESS - RECESS_DEPTH

# top recess inside the rim
gear = gear.cut(cyl(0, 0, RECESS_DIA / 2.0, z_floor, RECESS_DEPTH))

# central hub boss rising from the recess floor
hub_h = RECESS_DEPTH - HUB_TOP_BELOW
gear = gear.union(cyl(0, 0, HUB_DIA / 2.0, z_floor, hub_h))

# through bore
gear = gear.cut(cyl(0, 0, BORE_DIA / 2.0, 0, THICKNESS))

# lightening holes on a pitch circle (polar pattern)
for k in range(HOLE_COUNT):
    hx, hy = pol(HOLE_PCD_R, k * 2 * math.pi / HOLE_COUNT)
    gear = gear.cut(cyl(hx, hy, HOLE_DIA / 2.0, 0, THICKNESS))

result = gear
VIEW = {"azimuth": 45, "elevation": 26}
